import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 110.0          # plate width along X
L = 161.0          # plate length along Y
T = 1.7            # plate thickness
NOTCH_W = 53.25    # rectangular notch at the +X / -Y corner (X size)
NOTCH_D = 42.5     # notch size along Y
EDGE_R = 0.5       # rounding of the plate's top perimeter edges
CORNER_R = 0.5     # rounding of the plate's vertical corner edges

# standoffs
SO_D = 6.9         # outer diameter of the blind (threaded) standoffs
THRU_D = 7.4       # outer diameter of the through-hole standoffs
SO_H = 8.0         # standoff height above plate top
SO_HOLE = 2.5      # blind hole (tap drill) diameter
SO_HOLE_DEPTH = 6.5  # depth of the blind holes (cylindrical part)
SO_CSK = 0.7       # 45 deg chamfer on the blind hole mouth
THRU_HOLE = 3.8    # plain bore of the through-hole standoffs (through plate)
BASE_FILLET = 0.8  # root fillet of the through-hole standoffs

# blind-hole standoffs (x, y) measured from the plate's -X/-Y corner
BLIND_POS = [(16.5, 156.2), (16.5, 82.3), (61.4, 98.6), (58.2, 60.7)]
# through-hole standoffs with root fillet
THRU_POS = [(10.9, 24.8), (46.7, 5.4)]

# bent-up tabs with a rounded inner gusset along the +X edge
TAB_Y0 = [65.4, 131.2]   # start of each tab along Y
TAB_LEN = 24.0
TAB_H = 9.0        # wall height above plate top
TAB_T = 0.9        # wall thickness
GUS_W = 10.8       # gusset width (X) measured from the wall's inner face
GUS_H = 5.2        # gusset height above plate top
GUS_A = 6.0        # horizontal run of the rounded free edge
GUS_WALL_R = 0.8   # small concave blend gusset -> wall
WALL_TOP_R = 0.6   # rounding of the wall's top end corners

# ---------------- plate ----------------
plate = (
    cq.Workplane("XY")
    .polyline([
        (0, 0),
        (W - NOTCH_W, 0),
        (W - NOTCH_W, NOTCH_D),
        (W, NOTCH_D),
        (W, L),
        (0, L),
    ])
    .close()
    .extrude(T)
)
plate = plate.edges("|Z").fillet(CORNER_R)
plate = plate.faces(">Z").edges().fillet(EDGE_R)


# ---------------- tabs ----------------
def make_tab(y0):
    xw = W - TAB_T              # wall inner face
    xg = xw - GUS_W             # gusset free edge (foot on the plate)
    zt = T + GUS_H
    # circular arc from the foot (xg, T) to (xg + GUS_A, zt) with a
    # horizontal tangent at the top
    R = (GUS_A ** 2 + GUS_H ** 2) / (2.0 * GUS_H)
    cx, cz = xg + GUS_A, zt - R
    a0 = math.atan2(T - cz, xg - cx)
    a1 = math.pi / 2.0
    am = 0.5 * (a0 + a1)
    mid = (cx + R * math.cos(am), cz + R * math.sin(am))
    k = 1.0 - math.sqrt(0.5)
    zb = T - EDGE_R - 0.3        # sink the tab into the plate
    prof = (
        cq.Workplane("XZ", origin=(0, y0, 0))
        .moveTo(xg, zb)
        .lineTo(xg, T)
        .threePointArc(mid, (xg + GUS_A, zt))
        .lineTo(xw - GUS_WALL_R, zt)
        .threePointArc((xw - GUS_WALL_R * k, zt + GUS_WALL_R * k),
                       (xw, zt + GUS_WALL_R))
        .lineTo(xw, T + TAB_H)
        .lineTo(W, T + TAB_H)
        .lineTo(W, zb)
        .close()
        .extrude(-TAB_LEN)
    )
    # round the two top corners at the ends of the wall
    prof = prof.faces(">Z").edges("|X").fillet(WALL_TOP_R)
    return prof


part = plate
for y0 in TAB_Y0:
    part = part.union(make_tab(y0))

# ---------------- standoffs ----------------
def cyl(d, h, x, y, z):
    """vertical cylinder; its seam is turned to face +Y"""
    return (
        cq.Workplane("XY")
        .circle(d / 2.0)
        .extrude(h)
        .rotate((0, 0, 0), (0, 0, 1), 90)
        .translate((x, y, z))
    )


for (x, y) in BLIND_POS:
    part = part.union(cyl(SO_D, SO_H + 0.3, x, y, T - 0.3))
for (x, y) in THRU_POS:
    part = part.union(cyl(THRU_D, SO_H + 0.3, x, y, T - 0.3))

# root fillets on the through-hole standoffs
for (x, y) in THRU_POS:
    c45 = math.sqrt(0.5) * THRU_D / 2.0
    part = part.edges(
        cq.selectors.NearestToPointSelector((x - c45, y - c45, T))
    ).fillet(BASE_FILLET)

top_z = T + SO_H


def mouth_chamfer(x, y):
    return cq.Workplane().add(
        cq.Solid.makeCone(SO_HOLE / 2.0, SO_HOLE / 2.0 + SO_CSK + 0.2,
                          SO_CSK + 0.2,
                          cq.Vector(x, y, top_z - SO_CSK),
                          cq.Vector(0, 0, 1)))


# flat-bottomed blind holes with chamfered mouth
for (x, y) in BLIND_POS:
    hole = cyl(SO_HOLE, SO_HOLE_DEPTH + 1.0, x, y, top_z - SO_HOLE_DEPTH)
    part = part.cut(hole).cut(mouth_chamfer(x, y))

# through holes
for (x, y) in THRU_POS:
    hole = cyl(THRU_HOLE, T + SO_H + 2.0, x, y, -1.0)
    part = part.cut(hole)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
